import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
# Main body: L-shaped socket (footprint square with a notch at front-right)
BW = 60.4          # body size along X
BD = 60.9          # body size along Y
BH = 53.8          # body height (Z)
NOTCH_X0 = 42.05   # X where the front-right notch starts
NOTCH_Y1 = 18.8    # notch depth along Y (from the front face)

R_BL = 20.5        # back-left vertical corner radius
R_FL = 11.2        # front-left vertical corner radius
R_FR = 11.2        # front-right corner of the left column
R_IN = 2.4         # concave notch corner radius
R_RE = 5.4         # fillet on the top/bottom edges of the +X face

# L-shaped pocket open at the top
PK_X0 = 9.45
PK_X1 = 49.2
PK_Y0 = 7.45
PK_Y1 = 51.6
PK_NX = 32.6       # pocket notch corner X
PK_NY = 27.8       # pocket notch corner Y
FLOOR = 9.0        # floor thickness

# Boss + through hole underneath
BOSS_X = 20.75
BOSS_Y = 39.35
BOSS_R = 9.4
BOSS_H = 8.1
BOSS_HOLE_R = 5.6
FUNNEL_R = 13.0    # rounded lead-in where the hole meets the pocket floor

# Two small holes through the notch wall (along Y)
SH_X = 46.0
SH_Z = (48.8, 39.2)
SH_R = 1.7

# Mount (GoPro style, tilted about X)
M_Y = 36.4         # centre of the mount on the +X face
M_Z = 28.9
M_TILT = 30.0      # tilt about X (deg)
M_W = 34.4         # width (perpendicular to hole axis)
M_T = 14.6         # thickness (along hole axis)
M_XH = 19.3        # hole axis distance from the body face
M_HOLE_D = 8.4
M_TIP = 30.7       # lip (hook) tip distance from the face
M_LIP_T = 3.4      # lip thickness
M_LIP_R = 1.3      # rounding of the lip's top edge
M_SLOT_G = 3.5     # gap between the two fingers
M_SLOT_OFF = 0.45  # gap offset along the hole axis (towards +A)
M_SLOT_R1 = 11.5   # hub radius at the bottom of the finger gap
M_SLOT_HUB_DZ = 0.0  # hub centre offset from the hole axis (towards the lip)
M_SLOT_TOP = 12.0  # upper limit of the finger gap (width direction)
M_SLOT_X1 = 9.1   # upper part of the gap starts this far past the hole axis
M_SLOT_BACK = 8.0  # lower part of the gap runs back this far behind the axis


def nearest_edge(wp, pt):
    return wp.edges(cq.selectors.NearestToPointSelector(pt))


# ---------------------------------------------------------------------------
# Body
# ---------------------------------------------------------------------------
outer_pts = [
    (0, 0),
    (NOTCH_X0, 0),
    (NOTCH_X0, NOTCH_Y1),
    (BW, NOTCH_Y1),
    (BW, BD),
    (0, BD),
]
body = cq.Workplane("XY").polyline(outer_pts).close().extrude(BH)

zc = BH / 2
body = nearest_edge(body, (0, BD, zc)).fillet(R_BL)
body = nearest_edge(body, (0, 0, zc)).fillet(R_FL)
body = nearest_edge(body, (NOTCH_X0, 0, zc)).fillet(R_FR)
body = nearest_edge(body, (NOTCH_X0, NOTCH_Y1, zc)).fillet(R_IN)
ym = (NOTCH_Y1 + BD) / 2
body = nearest_edge(body, (BW, ym, BH)).fillet(R_RE)
body = nearest_edge(body, (BW, ym, 0)).fillet(R_RE)

# pocket
pk_pts = [
    (PK_X0, PK_Y0),
    (PK_NX, PK_Y0),
    (PK_NX, PK_NY),
    (PK_X1, PK_NY),
    (PK_X1, PK_Y1),
    (PK_X0, PK_Y1),
]
pocket = (
    cq.Workplane("XY")
    .workplane(offset=FLOOR)
    .polyline(pk_pts)
    .close()
    .extrude(BH)
)
body = body.cut(pocket)

# boss underneath + through hole
boss = (
    cq.Workplane("XY")
    .center(BOSS_X, BOSS_Y)
    .circle(BOSS_R)
    .extrude(-BOSS_H)
)
body = body.union(boss)
hole = (
    cq.Workplane("XY")
    .workplane(offset=-BOSS_H - 1)
    .center(BOSS_X, BOSS_Y)
    .circle(BOSS_HOLE_R)
    .extrude(FLOOR + BOSS_H + 2)
)
body = body.cut(hole)

# rounded (concave) lead-in from the pocket floor into the hole
funnel = (
    cq.Workplane("XZ")
    .moveTo(0, FLOOR - FUNNEL_R)
    .lineTo(BOSS_HOLE_R, FLOOR - FUNNEL_R)
    .radiusArc((BOSS_HOLE_R + FUNNEL_R, FLOOR), FUNNEL_R)
    .lineTo(BOSS_HOLE_R + FUNNEL_R, FLOOR + 1)
    .lineTo(0, FLOOR + 1)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((BOSS_X, BOSS_Y, 0))
)
body = body.cut(funnel)

# small holes in the notch wall
for z in SH_Z:
    h = (
        cq.Workplane("XZ")
        .workplane(offset=-NOTCH_Y1 + 1)
        .center(SH_X, z)
        .circle(SH_R)
        .extrude(-(PK_NY - NOTCH_Y1 + 2))
    )
    body = body.cut(h)

# ---------------------------------------------------------------------------
# Mount (built in a local frame: X = out of the face, Y = hole axis,
# Z = width direction with the lip on +Z)
# ---------------------------------------------------------------------------
Rm = M_W / 2
blk = (
    cq.Workplane("XY")
    .box(M_XH + 2, M_T, M_W, centered=(False, True, True))
    .translate((-2, 0, 0))
)
rnd = (
    cq.Workplane("XZ")
    .center(M_XH, 0)
    .circle(Rm)
    .extrude(M_T / 2, both=True)
)
lip = (
    cq.Workplane("XY")
    .box(M_TIP - M_XH, M_T, M_LIP_T, centered=(False, True, False))
    .translate((M_XH, 0, Rm - M_LIP_T))
)
lip = lip.edges("|Y and >X and >Z").fillet(M_LIP_R)
mount = blk.union(rnd).union(lip)

# gap between the fingers (leaves a hub around the hole axis)
slot_hi = (
    cq.Workplane("XY")
    .box(Rm + 10 - M_SLOT_X1, M_SLOT_G, Rm + 10 + M_SLOT_TOP,
         centered=(False, True, False))
    .translate((M_XH + M_SLOT_X1, 0, -Rm - 10))
)
slot_lo = (
    cq.Workplane("XY")
    .box(Rm + 10 + M_SLOT_BACK, M_SLOT_G, Rm + 10,
         centered=(False, True, False))
    .translate((M_XH - M_SLOT_BACK, 0, -Rm - 10))
)
slot_box = slot_hi.union(slot_lo)
hub = (
    cq.Workplane("XZ")
    .center(M_XH, M_SLOT_HUB_DZ)
    .circle(M_SLOT_R1)
    .extrude(M_T, both=True)
)
slot = slot_box.cut(hub).translate((0, M_SLOT_OFF, 0))
mount = mount.cut(slot)

mhole = (
    cq.Workplane("XZ")
    .center(M_XH, 0)
    .circle(M_HOLE_D / 2)
    .extrude(M_T, both=True)
)
mount = mount.cut(mhole)

mount = mount.rotate((0, 0, 0), (1, 0, 0), M_TILT).translate((BW, M_Y, M_Z))

result = body.union(mount).translate((-BW / 2, -BD / 2, -BH / 2))

VIEW = {"azimuth": 45, "elevation": 26}
